import cadquery as cq

# ---- driving dimensions (mm) ----
LEN_Y = 100.0        # long arm length (along +Y)
LEN_X = 61.7         # short arm length (along +X)
W = 13.0             # bar width (square section)
H = 12.8             # bar height
HOLE_D = 10.4        # vertical through-hole diameter
HOLE1_Y = 68.2       # long-arm hole centre (from Y=0)
HOLE2_X = 43.4       # short-arm hole centre (from X=0)
INNER_R = 1.0        # inner corner fillet of the L

# L-shaped outline in XY, extruded up Z
pts = [
    (0, 0),
    (LEN_X, 0),
    (LEN_X, W),
    (W, W),
    (W, LEN_Y),
    (0, LEN_Y),
]
body = cq.Workplane("XY").polyline(pts).close().extrude(H)

# round the inner vertical corner of the L
body = body.edges("|Z").edges(
    cq.selectors.NearestToPointSelector((W, W, H / 2))
).fillet(INNER_R)

# vertical through holes, one centred in each arm
hole_pts = [(W / 2, HOLE1_Y), (HOLE2_X, W / 2)]
cutter = (
    cq.Workplane("XY").workplane(offset=-1.0)
    .pushPoints(hole_pts)
    .circle(HOLE_D / 2)
    .extrude(H + 2.0)
)
body = body.cut(cutter)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
